import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Tandem-rotor transport helicopter (CH-47 style).  X = fuselage axis (nose at
# -X), Y = lateral, Z = up.  Units: mm.
# ---------------------------------------------------------------------------

# fuselage
NOSE_X = -69.5
TAIL_X = 66.5
HALF_W = 13.5
ROOF_Z = 2.2
BELLY_Z = -21.0
TOP_R = 8.0
BOT_R = 3.0
RAMP_TOP_Z = -3.0
NOSE_CAB_X = -56.0
RAMP_X0 = 41.5
BOAT_X0 = 40.0
TAIL_CH = 5.5

# sponsons
SP_X0, SP_X1 = -38.0, 48.0
SP_OUT = 18.0
SP_Z0, SP_Z1 = -19.2, -11.2

# rotors
FRONT_HUB = (-57.5, 0.0, 11.6)
REAR_HUB = (46.0, 0.0, 26.8)
BLADE_R = 77.0
BLADE_CHORD = 8.2
BLADE_T = 0.8
# (azimuth deg, droop deg) per blade
FRONT_BLADES = [(94.0, 5.9), (218.0, 12.8), (336.6, -2.9)]
REAR_BLADES = [(22.8, -0.5), (143.0, 12.7), (264.0, 7.3)]

# aft pylon
AP_TOP_Z = 22.3
AP_HW_REAR = 2.8
AP_HW_FRONT = 5.8

# engines
ENG_Y = 12.5
ENG_Z = 3.3

# landing gear
GEAR_X = (-27.0, 34.8)
GEAR_Y = 12.7
WHEEL_R = 2.6
WHEEL_W = 1.2
GROUND_Z = -28.3


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0)
            .translate(((x0 + x1) / 2, (y0 + y1) / 2, (z0 + z1) / 2)))


def cyl_x(x0, x1, r, y, z):
    return (cq.Workplane("YZ").workplane(offset=x0).center(y, z)
            .circle(r).extrude(x1 - x0))


def cyl_y(y0, y1, r, x, z):
    return (cq.Workplane("XZ").workplane(offset=-y1).center(x, z)
            .circle(r).extrude(y1 - y0))


def cyl_z(z0, z1, r, x, y):
    return (cq.Workplane("XY").workplane(offset=z0).center(x, y)
            .circle(r).extrude(z1 - z0))


def rrect_yz(x, y_half, z0, z1, r_top, r_bot):
    """rounded rectangle wire in a YZ plane at station x (same topology always)"""
    wp = (cq.Workplane("YZ").workplane(offset=x)
          .moveTo(-y_half + r_bot, z0)
          .lineTo(y_half - r_bot, z0)
          .radiusArc((y_half, z0 + r_bot), -r_bot)
          .lineTo(y_half, z1 - r_top)
          .radiusArc((y_half - r_top, z1), -r_top)
          .lineTo(-y_half + r_top, z1)
          .radiusArc((-y_half, z1 - r_top), -r_top)
          .lineTo(-y_half, z0 + r_bot)
          .radiusArc((-y_half + r_bot, z0), -r_bot)
          .close())
    return wp


def side_extrude(pts, half=40.0):
    """closed polyline in the XZ plane (x, z) extruded symmetric in Y"""
    return cq.Workplane("XZ").workplane(offset=-half).polyline(pts).close().extrude(2 * half)


# ---------------------------------------------------------------- fuselage
def fuselage():
    # side elevation (x, z): windshield slope and rear ramp
    side = (cq.Workplane("XZ").workplane(offset=-30)
            .moveTo(NOSE_X - 1.0, -25.0)
            .lineTo(NOSE_X - 1.0, -11.0)
            .lineTo(-67.3, -8.8)
            .lineTo(-60.0, 1.0)
            .lineTo(-57.0, ROOF_Z + 1.0)
            .lineTo(TAIL_X, ROOF_Z + 1.0)
            .lineTo(TAIL_X, RAMP_TOP_Z)
            .lineTo(RAMP_X0, BELLY_Z)
            .lineTo(RAMP_X0 - 2.0, -25.0)
            .close()
            .extrude(60))
    # plan (x, y): chamfered tail corners
    plan = (cq.Workplane("XY").workplane(offset=-30)
            .moveTo(-80.0, -HALF_W - 1)
            .lineTo(-80.0, HALF_W + 1)
            .lineTo(TAIL_X - TAIL_CH, HALF_W + 1)
            .lineTo(TAIL_X - TAIL_CH, HALF_W)
            .lineTo(TAIL_X, HALF_W - TAIL_CH)
            .lineTo(TAIL_X, -HALF_W + TAIL_CH)
            .lineTo(TAIL_X - TAIL_CH, -HALF_W)
            .lineTo(TAIL_X - TAIL_CH, -HALF_W - 1)
            .close()
            .extrude(60))
    # cabin: rounded-rectangle section
    cab = box(NOSE_CAB_X, TAIL_X + 5, -HALF_W, HALF_W, BELLY_Z, ROOF_Z)
    cab = cab.edges("|X and >Z").fillet(TOP_R).edges("|X and <Z").fillet(BOT_R)
    # nose: smooth loft from the cabin section to a small blunt tip
    ws = [rrect_yz(NOSE_CAB_X, HALF_W, BELLY_Z, ROOF_Z, TOP_R, BOT_R).ctx.pendingWires[0],
          rrect_yz(-64.0, 11.3, -20.2, -1.0, 6.0, 4.5).ctx.pendingWires[0],
          rrect_yz(NOSE_X, 6.5, -17.6, -9.2, 3.0, 3.2).ctx.pendingWires[0]]
    nose = cq.Workplane("XY").add(cq.Solid.makeLoft(ws, False))
    body = cab.union(nose).intersect(side).intersect(plan)
    # upper aft body narrows into the aft pylon through a concave sweep
    def sweep_sec(x, yp, zb, r):
        return (cq.Workplane("YZ").workplane(offset=x)
                .moveTo(yp, 40.0)
                .lineTo(yp, zb + r)
                .radiusArc((yp + r, zb), r)
                .lineTo(30.0, zb)
                .lineTo(30.0, 40.0)
                .close()).ctx.pendingWires[0]
    cutter = cq.Workplane("XY").add(cq.Solid.makeLoft(
        [sweep_sec(BOAT_X0, HALF_W + 0.5, RAMP_TOP_Z + 0.6, 8.0),
         sweep_sec(TAIL_X + 1.0, AP_HW_REAR - 0.1, RAMP_TOP_Z + 0.6, 3.0)], True))
    body = body.cut(cutter).cut(cutter.mirror("XZ"))
    return body


def wall_y(z):
    """outer half-width of the cabin section at height z"""
    zc = ROOF_Z - TOP_R
    if z > zc:
        return HALF_W - TOP_R + math.sqrt(max(TOP_R ** 2 - (z - zc) ** 2, 0.0))
    zc = BELLY_Z + BOT_R
    if z < zc:
        return HALF_W - BOT_R + math.sqrt(max(BOT_R ** 2 - (z - zc) ** 2, 0.0))
    return HALF_W


def ramp_panel_cut():
    """shallow tombstone-shaped recess outlining the loading ramp"""
    dx, dz = TAIL_X - RAMP_X0, RAMP_TOP_Z - BELLY_Z
    L = math.hypot(dx, dz)
    ang = math.degrees(math.atan2(dz, dx))
    u0, u1, hw, rc = 2.5, L - 1.0, 11.3, 7.5
    panel = (cq.Workplane("XY")
             .moveTo(u0, -hw)
             .lineTo(u1 - rc, -hw)
             .radiusArc((u1, -hw + rc), -rc)
             .lineTo(u1, hw - rc)
             .radiusArc((u1 - rc, hw), -rc)
             .lineTo(u0, hw)
             .close()
             .extrude(-3.0)
             .translate((0, 0, 0.4)))
    panel = panel.rotate((0, 0, 0), (0, 1, 0), -ang).translate((RAMP_X0, 0, BELLY_Z))
    return panel


def sponsons():
    out = None
    for sgn in (1, -1):
        # bulged section: meets the cabin wall at the top, bulges outward below
        sec = (cq.Workplane("YZ").workplane(offset=SP_X0 - 1)
               .moveTo(11.5, SP_Z1 + 0.8)
               .lineTo(HALF_W, SP_Z1 + 0.8)
               .spline([(16.2, SP_Z1 - 1.0), (SP_OUT, SP_Z1 - 3.9), (17.5, SP_Z0 + 1.6),
                        (15.5, SP_Z0)], includeCurrent=True)
               .lineTo(11.5, SP_Z0)
               .close()
               .extrude(SP_X1 - SP_X0 + 2))
        prof = side_extrude([(SP_X0, SP_Z1 + 1.5), (SP_X0 + 7.0, SP_Z0 - 0.5),
                             (30.0, SP_Z0 - 0.5), (SP_X1, -14.0), (SP_X1, SP_Z1 + 1.5)])
        plan = (cq.Workplane("XY").workplane(offset=-30)
                .moveTo(SP_X0 - 1, 10.0)
                .lineTo(SP_X0 + 3.0, SP_OUT - 2.0)
                .threePointArc((SP_X0 + 4.2, SP_OUT - 0.5), (SP_X0 + 6.0, SP_OUT + 0.5))
                .lineTo(SP_X1 - 4.0, SP_OUT + 0.5)
                .lineTo(SP_X1 + 1.0, 10.0)
                .close().extrude(40))
        sp = sec.intersect(prof).intersect(plan)
        if sgn < 0:
            sp = sp.mirror("XZ")
        out = sp if out is None else out.union(sp)
    return out


# ------------------------------------------------------------- pylons etc.
def front_pylon():
    side = (cq.Workplane("XZ").workplane(offset=-20)
            .moveTo(-61.0, 0.0)
            .lineTo(-60.6, 6.0)
            .threePointArc((-59.9, 8.9), (-58.0, 10.0))
            .lineTo(-48.5, 10.0)
            .lineTo(-38.5, 3.6)
            .lineTo(-38.5, 0.0)
            .close()
            .extrude(40))
    plan = (cq.Workplane("XY").workplane(offset=-5)
            .moveTo(-53.5, -6.5)
            .threePointArc((-60.0, 0.0), (-53.5, 6.5))
            .lineTo(-38.5, 5.5)
            .lineTo(-38.5, -5.5)
            .close()
            .extrude(20))
    # inclined upper sides (narrower at the top)
    sec = (cq.Workplane("YZ").workplane(offset=-70)
           .polyline([(-7.5, 0.0), (-7.5, 4.0), (-5.3, 10.5), (5.3, 10.5), (7.5, 4.0), (7.5, 0.0)])
           .close().extrude(40))
    p = side.intersect(plan).intersect(sec)
    # rotor head base fairing
    p = p.union(cq.Workplane("XY").workplane(offset=9.4).center(FRONT_HUB[0], 0)
                .polygon(8, 8.6).extrude(1.2))
    # long diagonal louvre slot on each side
    for sgn in (1, -1):
        slot = (cq.Workplane("XZ").workplane(offset=-10.0 if sgn > 0 else 5.6)
                .polyline([(-52.0, 7.0), (-43.5, 4.2), (-43.5, 3.5), (-52.0, 6.2)])
                .close().extrude(4.4))
        p = p.cut(slot)
    return p


def dorsal_tunnel():
    t = (cq.Workplane("YZ").workplane(offset=-44.0)
         .polyline([(-6.5, 0.0), (-6.5, 2.1), (-4.8, 3.1), (4.8, 3.1), (6.5, 2.1), (6.5, 0.0)])
         .close().extrude(72.0))
    groove = box(-44.0, 28.0, -0.45, 0.45, 2.7, 3.5)
    return t.cut(groove)


def aft_pylon():
    side = (cq.Workplane("XZ").workplane(offset=-20)
            .moveTo(20.0, 0.0)
            .lineTo(25.4, 4.5)
            .lineTo(30.6, 17.6)
            .threePointArc((32.8, 20.6), (36.5, 21.5))
            .lineTo(TAIL_X, AP_TOP_Z)
            .lineTo(TAIL_X, RAMP_TOP_Z)
            .lineTo(20.0, RAMP_TOP_Z)
            .close()
            .extrude(40))
    plan = (cq.Workplane("XY").workplane(offset=-5)
            .moveTo(28.0, -AP_HW_FRONT)
            .threePointArc((21.5, 0.0), (28.0, AP_HW_FRONT))
            .lineTo(TAIL_X, AP_HW_REAR)
            .lineTo(TAIL_X, -AP_HW_REAR)
            .close()
            .extrude(40))
    p = side.intersect(plan)
    # recessed vents / grilles on both sides (rounded-corner rectangles)
    vents = [(52.8, 14.9, 2.2, 5.0), (48.5, 10.0, 4.5, 2.0),
             (60.3, 13.4, 2.2, 1.8), (59.8, 6.45, 3.7, 1.8)]
    for (vx, vz, vl, vh) in vents:
        hw = AP_HW_FRONT - (AP_HW_FRONT - AP_HW_REAR) * (vx - 28.0) / (TAIL_X - 28.0)
        c = (cq.Workplane("XZ").workplane(offset=-10).center(vx, vz).rect(vl, vh)
             .extrude(20).edges("|Y").fillet(0.35))
        core = box(vx - vl, vx + vl, -hw + 0.5, hw - 0.5, vz - 5, vz + 5)
        p = p.cut(c.cut(core))
    # rotor head base fairing
    base = (cq.Workplane("XY").workplane(offset=AP_TOP_Z - 1.0)
            .center(REAR_HUB[0], 0).polygon(8, 9.0).extrude(1.6))
    return p.union(base)


def engine(sgn):
    y = sgn * ENG_Y
    z = ENG_Z
    e = cyl_x(30.4, 36.5, 3.9, y, z).faces("<X").edges().fillet(1.6)
    cone = (cq.Workplane("YZ").workplane(offset=36.5).center(y, z).circle(3.8)
            .workplane(offset=9.0).circle(2.5).loft())
    ex = cyl_x(45.4, 49.2, 2.35, y, z)
    e = e.union(cone).union(ex)
    # intake bullet
    e = e.union(cq.Workplane("XY").sphere(1.6).translate((30.6, y, z)))
    # mount fairing from pylon side to engine top
    mount = (cq.Workplane("YZ").workplane(offset=31.0)
             .polyline([(0.0, 4.5), (y, z + 2.6), (y, z + 4.0), (0.0, 6.8)])
             .close().extrude(12.0))
    e = e.union(mount)
    # exhaust opening
    e = e.cut(cyl_x(47.8, 49.5, 1.6, y, z))
    return e


# ------------------------------------------------------------------ rotors
def blade(az, droop):
    """rotor blade: straight root panel at a small droop, then an outer panel that
    curves smoothly downward (revolved band) so the tip reaches the measured droop"""
    r0, r1 = 4.5, 8.5
    rs = r1 + 4.5                       # start of full chord / start of the bend
    L = BLADE_R - rs
    if droop > 1.0:
        d1 = math.radians(0.7 * droop)
        target = BLADE_R * math.sin(math.radians(droop))
        lo, hi = 1e-4, 1.2
        for _ in range(60):             # bisection on the bend angle
            th = 0.5 * (lo + hi)
            rc = L / th
            drop = rs * math.sin(d1) + rc * (math.cos(d1) - math.cos(d1 + th))
            if drop > target:
                hi = th
            else:
                lo = th
        th = 0.5 * (lo + hi)
    else:
        d1, th = math.radians(droop), 0.0
    root = box(r0, r1 + 0.5, -1.6, 1.6, -BLADE_T / 2, BLADE_T / 2)
    taper = (cq.Workplane("XY").workplane(offset=-BLADE_T / 2)
             .polyline([(r1, -1.6), (rs, -BLADE_CHORD / 2), (rs + 0.01, -BLADE_CHORD / 2),
                        (rs + 0.01, BLADE_CHORD / 2), (rs, BLADE_CHORD / 2), (r1, 1.6)])
             .close().extrude(BLADE_T))
    if th > 1e-3:
        rc = L / th
        outer = (cq.Workplane("YZ").workplane(offset=rs).rect(BLADE_CHORD, BLADE_T)
                 .revolve(math.degrees(th), (0, -rc), (1, -rc)))
    else:
        outer = box(rs, BLADE_R, -BLADE_CHORD / 2, BLADE_CHORD / 2, -BLADE_T / 2, BLADE_T / 2)
    # blade grip / damper sleeve
    grip = cq.Workplane("YZ").workplane(offset=1.5).circle(1.0).extrude(8.5)
    cuff = cq.Workplane("YZ").workplane(offset=6.5).circle(1.35).extrude(2.5)
    damper = cq.Workplane("YZ").workplane(offset=2.0).center(1.2, 0.5).circle(0.55).extrude(6.0)
    b = root.union(taper).union(outer).union(grip).union(cuff).union(damper)
    b = b.rotate((0, 0, 0), (0, 1, 0), math.degrees(d1))
    b = b.rotate((0, 0, 0), (0, 0, 1), az)
    return b


def rotor_head(hub, blades, mast_z0, top_h):
    hx, hy, hz = hub
    head = cyl_z(mast_z0, hz - 1.0, 1.7, hx, hy)                      # mast
    head = head.union(cyl_z(hz - 2.0, hz - 1.3, 3.8, hx, hy))          # swashplate
    head = head.union(cyl_z(hz - 1.3, hz + 1.0, 2.6, hx, hy))          # hub body
    head = head.union(cyl_z(hz + 1.0, hz + top_h, 2.0, hx, hy))        # upper head / cap
    for az, droop in blades:
        head = head.union(blade(az, droop).translate((hx, hy, hz)))

        # pitch link
        a = math.radians(az + 40.0)
        head = head.union(cyl_z(hz - 2.5, hz, 0.35, hx + 3.2 * math.cos(a), hy + 3.2 * math.sin(a)))
    return head


# ------------------------------------------------------------ landing gear
def gear(x, sgn, front):
    y = sgn * GEAR_Y
    zc = GROUND_Z + WHEEL_R
    g = None
    for dy in (-0.95, 0.95):
        w = cyl_y(y + dy - WHEEL_W / 2, y + dy + WHEEL_W / 2, WHEEL_R, x, zc)
        g = w if g is None else g.union(w)
    g = g.union(cyl_y(y - 1.7, y + 1.7, 0.9, x, zc))                   # hub / axle
    top_x = x - 3.5 if front else x - 2.0
    top_z = SP_Z0 + 0.8
    ln = math.hypot(top_x - x, top_z - zc)
    strut = cq.Workplane("XY").workplane(offset=zc).center(x, y).circle(0.6).extrude(ln)
    lean = math.degrees(math.atan2(top_x - x, top_z - zc))
    strut = strut.rotate((x, y, zc), (x, y + 1, zc), lean)
    g = g.union(strut)
    return g


# ----------------------------------------------------------------- details
def side_rail(x0, x1, z, sgn, n, stand=2.2):
    """handrail: a thin bar held off the wall with n angled fins"""
    yw = sgn * (wall_y(z) - 0.8)
    yo = sgn * (wall_y(z) + stand)
    bar = box(x0, x1, min(yo - sgn * 0.6, yo), max(yo - sgn * 0.6, yo), z - 0.3, z + 0.3)
    r = bar
    for i in range(n):
        px = x0 + 0.4 + i * (x1 - x0 - 0.8) / (n - 1)
        post = box(px - 0.22, px + 0.22, min(yw, yo), max(yw, yo), z - 0.3, z + 0.3)
        fin = (box(px - 0.2, px + 0.2, -0.3, 0.3, 0.0, 1.8)
               .rotate((0, 0, 0), (1, 0, 0), -sgn * 35.0)
               .translate((0, yo - sgn * 0.3, z)))
        r = r.union(post).union(fin)
    return r


def gun(sgn, z):
    """door / window machine gun: receiver, long barrel forward, ammo box, mount arm"""
    y = sgn * 15.4
    rec = box(-45.5, -42.0, y - 0.9, y + 0.9, z - 0.9, z + 0.9)
    barrel = cyl_x(-54.5, -45.5, 0.38, y, z + 0.2)
    jacket = cyl_x(-48.5, -45.5, 0.6, y, z + 0.2)
    grip = box(-42.4, -41.4, y - 0.3, y + 0.3, z - 2.0, z - 0.9)
    ammo = box(-45.0, -43.0, y - 0.8 - sgn * 1.4, y + 0.8 - sgn * 1.4, z - 2.4, z - 0.8)
    arm = box(-44.0, -43.2, min(y, sgn * (wall_y(z) - 1.0)), max(y, sgn * (wall_y(z) - 1.0)),
              z - 0.35, z + 0.35)
    return rec.union(barrel).union(jacket).union(grip).union(ammo).union(arm)


def window_cuts(part):
    depth = 0.45
    # plan-view approximation of the nose surface, moved inward by the recess depth
    surf = [(-72.0, 5.0), (-69.0, 7.8), (-67.0, 9.4), (-64.0, 10.9), (-60.0, 12.4),
            (-56.0, HALF_W - 0.1), (-48.0, HALF_W)]
    inner = [(x, y - depth) for (x, y) in surf]
    region = (cq.Workplane("XY").workplane(offset=-30)
              .polyline(inner + [(-48.0, 25.0), (-72.0, 25.0)]).close().extrude(40))
    quads = ([(-65.6, -8.6), (-61.4, -2.2), (-56.6, -2.2), (-56.6, -8.6)],
             [(-67.4, -10.0), (-60.0, -10.0), (-60.0, -15.2), (-66.6, -15.8)],
             [(-55.4, -2.6), (-51.4, -2.6), (-51.4, -6.8), (-55.4, -6.8)])
    cut_all = None
    for quad in quads:
        prism = (cq.Workplane("XZ").workplane(offset=-25.0)
                 .polyline(quad).close().extrude(25.0))
        c = prism.intersect(region)
        cut_all = c if cut_all is None else cut_all.union(c)
    part = part.cut(cut_all).cut(cut_all.mirror("XZ"))
    # windshield panes on the sloped front
    ang = math.degrees(math.atan2(9.8, 7.3))
    for (y0, y1) in ((0.6, 7.4), (-7.4, -0.6)):
        pane = (box(1.4, 10.2, y0, y1, -depth, 3.0)
                .rotate((0, 0, 0), (0, 1, 0), -ang)
                .translate((-67.3, 0, -8.8)))
        part = part.cut(pane)
    return part


def build():
    part = fuselage()
    part = part.cut(ramp_panel_cut())
    part = part.union(sponsons())
    part = part.union(front_pylon())
    part = part.union(dorsal_tunnel())
    part = part.union(aft_pylon())
    for sgn in (1, -1):
        part = part.union(engine(sgn))
    # door recess on -Y side
    part = part.cut(box(-45.5, -39.0, -HALF_W - 1, -HALF_W + 0.6, -10.5, -4.5))
    # cockpit windows (shallow recesses)
    part = window_cuts(part)
    # rotor heads
    part = part.union(rotor_head(FRONT_HUB, FRONT_BLADES, 9.0, 2.8))
    part = part.union(rotor_head(REAR_HUB, REAR_BLADES, 21.5, 1.1))
    # landing gear
    for i, gx in enumerate(GEAR_X):
        for sgn in (1, -1):
            part = part.union(gear(gx, sgn, i == 0))
    # rails / steps
    for sgn in (1, -1):
        part = part.union(side_rail(-48.0, -30.0, -0.6, sgn, 6))
        part = part.union(side_rail(15.5, 31.0, -2.8, sgn, 5))
    # guns
    part = part.union(gun(-1, -12.0))
    part = part.union(gun(1, -6.0))
    # blade antenna on the dorsal tunnel
    ant = (cq.Workplane("XZ").workplane(offset=-0.15)
           .polyline([(-10.5, 2.5), (-12.0, 4.6), (-11.3, 4.6), (-9.3, 2.5)]).close().extrude(0.3))
    part = part.union(ant).union(box(-12.6, -10.6, -1.1, 1.1, 4.4, 4.8))
    # pitot probes
    for sgn in (1, -1):
        part = part.union(cyl_x(NOSE_X - 3.0, NOSE_X + 4.0, 0.3, sgn * 6.0, -10.3))
    # belly bumps / antennas
    part = part.union(box(-16.0, -13.0, 2.0, 8.0, BELLY_Z - 1.2, BELLY_Z + 0.5))
    part = part.union(box(22.5, 25.0, -3.0, 3.0, BELLY_Z - 1.0, BELLY_Z + 0.5))
    # cargo hook (detached)
    part = part.union(cq.Workplane("XY").sphere(0.6).translate((-3.0, 0.0, -27.6)))
    return part


result = build()
